import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 170.0        # overall width (X), outer face to outer face of uprights
D = 50.0         # depth (Y)
H = 108.0        # overall height (Z)
T = 8.5          # plate thickness (base and uprights)
R_IN = 13.0      # inner bend fillet radius
R_TOP = D / 2.0  # full round at top of uprights

# bearing boss on the outer face of each upright
BOSS_R0 = 15.3   # boss radius at the plate
BOSS_R1 = 12.5   # boss radius at its top (conical / chamfered side)
BOSS_H = 2.6     # boss protrusion
CB_R = 9.7       # counterbore radius (bearing seat)
CB_DEPTH = 6.5   # counterbore depth measured from boss top
HOLE_R = 6.45    # through hole radius
Z_AXIS = H - R_TOP  # height of bearing axis (concentric with top round)

# motor-mount pattern on the +X upright
SLOT_HOLE_W = 19.2   # stadium hole width (Y)
SLOT_HOLE_H = 24.0   # stadium hole height (Z)
Z_MOTOR = 41.3       # centre height of stadium hole
SLOT_DY = 13.3       # slot offset in Y
SLOT_DZ = 13.4       # slot offset in Z
SLOT_L = 8.2         # slot length (Z)
SLOT_W = 3.2         # slot width

BASE_HOLE_D = 5.5    # small hole in the middle of the base

xo = W / 2.0         # outer face of upright
xi = W / 2.0 - T     # inner face of upright


def seam_to(solid, p, d, u_target):
    """Rotate a solid of revolution about its axis so its seam faces u_target
    (purely cosmetic: keeps seam lines on the hidden side)."""
    for e in solid.Edges():
        if e.geomType() == "LINE":
            c = e.Center() - p
            u0 = c - d * c.dot(d)
            if u0.Length < 1e-6:
                continue
            u0 = u0.normalized()
            ut = (u_target - d * u_target.dot(d)).normalized()
            ang = math.degrees(math.atan2(u0.cross(ut).dot(d), u0.dot(ut)))
            return solid.rotate(p, p + d, ang)
    return solid


# ---------------- U-channel body ----------------
# profile in XZ, extruded symmetrically along Y
u_body = (
    cq.Workplane("XZ")
    .moveTo(-xo, 0)
    .lineTo(xo, 0)
    .lineTo(xo, H)
    .lineTo(xi, H)
    .lineTo(xi, T)
    .lineTo(-xi, T)
    .lineTo(-xi, H)
    .lineTo(-xo, H)
    .close()
    .extrude(D / 2.0, both=True)
)
# fillet the two inner bend edges (parallel to Y at x=+-xi, z=T)
u_body = u_body.edges("|Y").edges(
    cq.selectors.BoxSelector((-xi - 0.1, -D, T - 0.1), (xi + 0.1, D, T + 0.1))
).fillet(R_IN)

# full-round tops: intersect with a YZ side profile (rectangle + semicircle)
side = (
    cq.Workplane("YZ", origin=(-W, 0, 0))
    .moveTo(-D / 2.0, 0)
    .lineTo(D / 2.0, 0)
    .lineTo(D / 2.0, Z_AXIS)
    .threePointArc((0, H), (-D / 2.0, Z_AXIS))
    .close()
    .extrude(2 * W)
)
body = u_body.intersect(side)

# ---------------- bearing bosses with counterbored bores ----------------
for sgn in (1, -1):
    d = cq.Vector(sgn, 0, 0)
    p = cq.Vector(sgn * xo, 0, Z_AXIS)
    hide_out = cq.Vector(0, sgn, -1)      # boss seam on the side away from camera
    hide_in = cq.Vector(0, -1, 1)         # bore seams on the near side of the bore
    cone = cq.Solid.makeCone(BOSS_R0, BOSS_R1, BOSS_H, p, d)
    cone = seam_to(cone, p, d, hide_out)
    body = body.union(cq.Workplane().add(cone))
    top = p + d * BOSS_H
    cb = cq.Solid.makeCylinder(CB_R, CB_DEPTH + 0.5, top + d * 0.5, -d)
    cb = seam_to(cb, top, d, hide_in)
    body = body.cut(cq.Workplane().add(cb))
    th = cq.Solid.makeCylinder(HOLE_R, T + BOSS_H + 2.0, top + d * 1.0, -d)
    th = seam_to(th, top, d, hide_in)
    body = body.cut(cq.Workplane().add(th))

# ---------------- motor mount cut-outs on +X upright ----------------
stadium = (
    cq.Workplane("YZ", origin=(xi - 1.0, 0, 0))
    .center(0, Z_MOTOR)
    .slot2D(SLOT_HOLE_H, SLOT_HOLE_W, angle=90)
    .extrude(T + 2.0)
)
body = body.cut(stadium)

slot_pts = [(sy * SLOT_DY, Z_MOTOR + sz * SLOT_DZ) for sy in (1, -1) for sz in (1, -1)]
slots = (
    cq.Workplane("YZ", origin=(xi - 1.0, 0, 0))
    .pushPoints(slot_pts)
    .slot2D(SLOT_L, SLOT_W, angle=90)
    .extrude(T + 2.0)
)
body = body.cut(slots)

# ---------------- base hole ----------------
base_hole = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .circle(BASE_HOLE_D / 2.0)
    .extrude(T + 2.0)
)
body = body.cut(base_hole)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
